"""Novelty coin "In Munzwurf We Trust".

A flat disc with a raised rim on both faces; inside each rim the field is
recessed.  The top field carries a Wikipedia-style serif W in relief plus the
legend "In Munzwurf We Trust" set along the lower arc; the underside field
carries a serif M with a short straight line of lettering below it.
Glyph outlines are built from straight stroke / serif polygons, fused into one
planar face, corner-rounded with 2D fillets (serif brackets, rounded serif
tips) and extruded.
"""
import math
import cadquery as cq
from OCP.BRepFilletAPI import BRepFilletAPI_MakeFillet2d

# ---------------- driving dimensions (mm) ----------------
R = 20.0              # coin radius
T = 2.9               # coin thickness (rim to rim)
RIM_W = 2.05          # width of the raised rim ring
POCKET = 0.37         # depth of the recessed field inside the rim (each face)
RELIEF = 0.88         # height of W / lettering above the recessed field

# W logo geometry, normalised to the coin radius
W_YB = -0.492         # bottom of the W (vertex feet)
W_YS = 0.350          # underside of the serifs
W_YT = 0.393          # top of the serifs
W_THICK = 0.20        # horizontal width of the thick strokes
W_THIN = 0.078        # horizontal width of the thin strokes
W_K_THICK = -0.45     # slope dX/dY of the thick strokes
W_S1_LEFT_TOP = -0.603   # stroke 1 (thick): left edge at the serif underside
W_S2_RIGHT_BOT = -0.159  # stroke 2 (thin): right edge at the foot
W_S2_SLOPE = 0.52        # stroke 2 slope dX/dY
W_S3_LEFT_TOP = -0.212   # stroke 3 (thick): left edge at the serif underside
W_S4_RIGHT_BOT = 0.231   # stroke 4 (thin): right edge at the foot ...
W_S4_RIGHT_TOP = 0.5915  # ... and at the serif underside
SERIFS = [(-0.680, -0.326), (-0.281, 0.056), (0.096, 0.377), (0.410, 0.688)]
W_BRACKET = 0.060      # tangent length of the serif brackets

# M logo on the underside (drawn in top-view coordinates, normalised)
M_YB = -0.492         # bottom of the middle vertex
M_FOOT_YB = -0.470    # bottom of the two feet
M_YT = 0.404          # top of the head serifs
M_SERIF = 0.045       # serif thickness
M_LSTEM = (-0.470, -0.355)   # thin left stem
M_RSTEM = (0.270, 0.460)     # thick right stem
M_FEET = [(-0.568, -0.235), (0.178, 0.568)]
M_HEAD_L = -0.530     # outer end of the top-left serif
M_HEAD_R = 0.575      # outer end of the top-right serif
M_NOTCH = (0.026, -0.220)    # apex of the middle V notch
M_K_THICK = -0.430    # slope dX/dY of the thick diagonal (both edges)
M_K_THIN_UL = 0.447   # slope of the upper-left edge of the thin diagonal
M_K_THIN_LR = 0.345   # slope of its lower-right edge (the stroke tapers)
M_LCOUNTER = (-0.355, 0.190)   # apex of the left counter (on thick diagonal LL edge)
M_RCOUNTER = (0.270, 0.176)    # apex of the right counter (on thin diagonal LR edge)
M_BRACKET = 0.090      # tangent length of the serif brackets

# lettering
TEXT_TOP = "In Munzwurf We Trust"
TEXT_R = 0.84         # baseline radius (normalised)
TEXT_SIZE = 0.105     # font size (normalised)
TEXT_BOT = "Munzwurf"  # small straight line of text under the M (underside)
TEXT_BOT_Y = -0.648   # its baseline (normalised, top-view coordinates)
TEXT_BOT_X = -0.010   # its centre
TEXT_BOT_SIZE = 0.110

VIEW = {"azimuth": 45, "elevation": 26}


def _line_x(x0, y0, slope, y):
    return x0 + (y - y0) * slope


def _isect(xa, ya, sa, xb, yb, sb):
    # lines x = xa + (y-ya)*sa and x = xb + (y-yb)*sb
    y = (xb - yb * sb - xa + ya * sa) / (sa - sb)
    return (xa + (y - ya) * sa, y)


def w_polygons(s=1.0):
    yb, ys, yt = W_YB, W_YS, W_YT
    k_thick = W_K_THICK
    # stroke 1 (thick) / stroke 2 (thin) -> first V
    s1_left_top = W_S1_LEFT_TOP
    s2_right_bot = W_S2_RIGHT_BOT
    s2_slope = W_S2_SLOPE
    # stroke 3 (thick) / stroke 4 (thin) -> second V
    s3_left_top = W_S3_LEFT_TOP
    s4_right_bot = W_S4_RIGHT_BOT
    s4_slope = (W_S4_RIGHT_TOP - s4_right_bot) / (ys - yb)

    ym = 0.5 * (ys + yt)   # strokes run up into the serifs
    polys = []
    # V1
    p1 = (_line_x(s1_left_top, ys, k_thick, yb), yb)
    p2 = (_line_x(s1_left_top, ys, k_thick, ym), ym)
    p3 = (p2[0] + W_THICK, ym)
    p4 = _isect(s1_left_top + W_THICK, ys, k_thick, s2_right_bot - W_THIN, yb, s2_slope)
    p6 = (_line_x(s2_right_bot, yb, s2_slope, ym), ym)
    p5 = (p6[0] - W_THIN, ym)
    p7 = (s2_right_bot, yb)
    polys.append([p7, p6, p5, p4, p3, p2, p1])  # counter-clockwise
    # V2
    q1 = (_line_x(s3_left_top, ys, k_thick, yb), yb)
    q2 = (_line_x(s3_left_top, ys, k_thick, ym), ym)
    q3 = (q2[0] + W_THICK, ym)
    q4 = _isect(s3_left_top + W_THICK, ys, k_thick, s4_right_bot - W_THIN, yb, s4_slope)
    q6 = (_line_x(s4_right_bot, yb, s4_slope, ym), ym)
    q5 = (q6[0] - W_THIN, ym)
    q7 = (s4_right_bot, yb)
    polys.append([q7, q6, q5, q4, q3, q2, q1])
    # serifs (overlap the stroke tops a little)
    for a, b in SERIFS:
        polys.append([(a, ys), (b, ys), (b, yt), (a, yt)])
    return [[(x * s, y * s) for x, y in p] for p in polys]


def m_polygons(s=1.0):
    yb, yf, yt, st = M_YB, M_FOOT_YB, M_YT, M_SERIF
    ys = yt - st
    yi = yt - 0.5 * st   # diagonals run up into the head serifs
    kk = M_K_THICK
    x_ll = lambda y: _line_x(M_LCOUNTER[0], M_LCOUNTER[1], kk, y)
    x_ur = lambda y: _line_x(M_NOTCH[0], M_NOTCH[1], kk, y)
    x_ul = lambda y: _line_x(M_NOTCH[0], M_NOTCH[1], M_K_THIN_UL, y)
    x_lr = lambda y: _line_x(M_RCOUNTER[0], M_RCOUNTER[1], M_K_THIN_LR, y)
    polys = []
    # stems
    for a, b in (M_LSTEM, M_RSTEM):
        polys.append([(a, yf + 0.5 * st), (b, yf + 0.5 * st), (b, yi), (a, yi)])
    # middle V (thick diagonal + thin diagonal), counter-clockwise
    polys.append([(x_ll(yb), yb), (x_lr(yb), yb), (x_lr(yi), yi), (x_ul(yi), yi),
                  M_NOTCH, (x_ur(yi), yi), (x_ll(yi), yi)])
    # feet
    for a, b in M_FEET:
        polys.append([(a, yf), (b, yf), (b, yf + st), (a, yf + st)])
    # head serifs
    polys.append([(M_HEAD_L, ys), (x_ur(ys), ys), (x_ur(yt), yt), (M_HEAD_L, yt)])
    polys.append([(x_ul(ys), ys), (M_HEAD_R, ys), (M_HEAD_R, yt), (x_ul(yt), yt)])
    return [[(x * s, y * s) for x, y in p] for p in polys]


def glyph_face(polys, s, serif_levels, end_xs, d_bracket, d_tip, d_tip_in, d_other=0.010):
    """Fuse the stroke / serif polygons into one planar face and round its
    corners with 2D fillets.  Each corner gets a wanted tangent length
    (bracket under a serif, rounded serif tip, small elsewhere); the radius
    follows from the corner angle, and tangent lengths are scaled down where
    two fillets would collide on a short edge."""
    faces = []
    for pts in polys:
        faces.append(cq.Face.makeFromWires(cq.Wire.makePolygon(
            [cq.Vector(x, y, 0) for x, y in pts], close=True)))
    f = faces[0].fuse(*faces[1:]).clean()
    face = max(f.Faces(), key=lambda q: q.Area())

    verts = face.Vertices()
    edges = face.Edges()
    key = lambda v: (round(v.X, 6), round(v.Y, 6))
    vinfo = {}
    for v in verts:
        vinfo[key(v)] = {"v": v, "nb": [], "d": 0.0}
    elen = []
    for e in edges:
        a, b = e.startPoint(), e.endPoint()
        ka, kb = (round(a.x, 6), round(a.y, 6)), (round(b.x, 6), round(b.y, 6))
        vinfo[ka]["nb"].append((b.x - a.x, b.y - a.y))
        vinfo[kb]["nb"].append((a.x - b.x, a.y - b.y))
        elen.append((ka, kb, e.Length()))
    # wanted tangent lengths
    for k, inf in vinfo.items():
        x, y = k
        on_serif = any(abs(y - lv * s) < 1e-6 for lv in serif_levels)
        is_end = any(abs(x - e * s) < 1e-6 for e in end_xs)
        if on_serif and not is_end:
            inf["d"] = d_bracket * s
        elif is_end and on_serif:
            inf["d"] = d_tip_in * s
        elif is_end:
            inf["d"] = d_tip * s
        else:
            inf["d"] = d_other * s
    # keep neighbouring fillets apart on short edges
    for _ in range(3):
        for ka, kb, L in elen:
            da, db = vinfo[ka]["d"], vinfo[kb]["d"]
            if da + db > 0.92 * L:
                f_ = 0.92 * L / (da + db)
                vinfo[ka]["d"], vinfo[kb]["d"] = da * f_, db * f_
    mk = BRepFilletAPI_MakeFillet2d(face.wrapped)
    for k, inf in vinfo.items():
        (ux, uy), (wx, wy) = inf["nb"][:2]
        lu, lw = math.hypot(ux, uy), math.hypot(wx, wy)
        c = max(-1.0, min(1.0, (ux * wx + uy * wy) / (lu * lw)))
        phi = math.acos(c)
        r = inf["d"] * math.tan(phi / 2.0)
        if r > 1e-4:
            mk.AddFillet(inf["v"].wrapped, r)
    mk.Build()
    return cq.Face(mk.Shape())


def w_face(s):
    ends = [e for ab in SERIFS for e in ab]
    return glyph_face(w_polygons(s), s, [W_YS], ends, W_BRACKET, 0.022, 0.010)


def m_face(s):
    ends = [e for ab in M_FEET for e in ab] + [M_HEAD_L, M_HEAD_R]
    return glyph_face(m_polygons(s), s, [M_YT - M_SERIF, M_FOOT_YB + M_SERIF], ends, M_BRACKET, 0.022, 0.010)


def relief_from_face(face, z0, h, flip=False):
    solid = cq.Solid.extrudeLinear(face, cq.Vector(0, 0, h))
    if flip:
        solid = solid.mirror("XY")
    return solid.translate(cq.Vector(0, 0, z0))


def arc_text(txt, r, ang_list, size, h, z0, flip=False):
    out = []
    for ch, ang in zip(txt, ang_list):
        if ch == " ":
            continue
        t = cq.Workplane("XY").text(ch, size, h, combine=False, font="DejaVu Sans",
                                    halign="center", valign="bottom")
        sol = t.val()
        sol = sol.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), ang + 90.0)
        sol = sol.translate(cq.Vector(r * math.cos(math.radians(ang)),
                                      r * math.sin(math.radians(ang)), 0))
        if flip:
            sol = sol.mirror("XY")
        out.append(sol.translate(cq.Vector(0, 0, z0)))
    return out


# ---------------- coin body ----------------
R_IN = R - RIM_W
SEAM = 45.0           # put the circular seams on the silhouette of the default view
wp = cq.Workplane("XY").transformed(rotate=(0, 0, SEAM))
body = wp.circle(R).extrude(T).translate((0, 0, -T / 2))
body = body.cut(wp.workplane(offset=T / 2 - POCKET).circle(R_IN).extrude(POCKET + 1))
body = body.cut(wp.workplane(offset=-T / 2 - 1).circle(R_IN).extrude(POCKET + 1))

z_top = T / 2 - POCKET
z_bot = -T / 2 + POCKET

# ---------------- top face: W + lettering ----------------
wf = w_face(R)
top_w = relief_from_face(wf, z_top - 0.01, RELIEF + 0.01)
body = body.union(cq.Workplane().add(top_w))

# character angles along the bottom arc (degrees, counter-clockwise from +X)
ANG_TOP = [-145.6, -142.3, None, -129.4, -123.9, -118.3, -112.8, -107.2, -101.7, -96.1, -90.6,
           None, -74.4, -68.1, None, -55.6, -50.4, -45.1, -39.9, -34.6]
chars = [c for c, a in zip(TEXT_TOP, ANG_TOP) if a is not None]
angs = [a for a in ANG_TOP if a is not None]
try:
    for sol in arc_text(chars, TEXT_R * R, angs, TEXT_SIZE * R, RELIEF + 0.01, z_top - 0.01):
        body = body.union(cq.Workplane().add(sol))
except Exception:
    pass

# ---------------- bottom face: M ----------------
mb = m_face(R)
bot_m = relief_from_face(mb, z_bot + 0.01, RELIEF + 0.01, flip=True)
body = body.union(cq.Workplane().add(bot_m))

# lettering under the M
try:
    tb = cq.Workplane("XY").text(TEXT_BOT, TEXT_BOT_SIZE * R, RELIEF + 0.01, combine=False,
                                 font="DejaVu Sans", halign="center", valign="bottom").val()
    tb = tb.mirror("XY").translate(cq.Vector(TEXT_BOT_X * R, TEXT_BOT_Y * R, z_bot + 0.01))
    body = body.union(cq.Workplane().add(tb))
except Exception:
    pass

result = body
